import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# shaft (oval, vertical)
SHAFT_A = 7.5          # half width along X
SHAFT_B = 9.75         # half length along Y
SHAFT_TOP = 100.0

# hood (C-shaped thin wall around a vertical axis in front of the shaft)
C_Y = -33.8            # Y position of the hood axis
HOOD_R_OUT = 26.0      # outer radius at the bottom
HOOD_T = 1.6           # wall thickness
HOOD_TOP = 55.8        # top height of the hood
HOOD_R_OUT_TOP = 22.0  # outer radius at the top (wall leans inward)
HOOD_Z_BEND = 30.0     # the wall is (nearly) vertical up to here
OPEN_HALF = 45.0       # half angle of the opening toward -Y

# top edge profile of the hood seen from the side (Y, Z)
END_Z = 37.0           # height of the vertical end edges
END_Y = -51.3
TOP_FLAT_Y = -25.4
# measured side silhouette of the rounded top corner (Y, Z)
TOP_CURVE = [(-29.0, 55.3), (-36.3, 52.3), (-43.6, 46.9), (-50.2, 39.3)]

# neck under the shaft, tapering from a rounded block into the oval shaft
COL_HX = 17.2          # half width of the block the neck is trimmed to
COL_Y0 = -18.0         # front of that block (hidden inside the hood ring)
COL_Y1 = 10.2          # back of that block
COL_R = 6.0
NECK_BASE = (23.0, 19.0, -3.0)      # elliptic section at z=0 (a, b, y-centre)
NECK_MID = (14.2, 13.2, -1.8)       # elliptic section half way up
NECK_MID_Z = 34.0
FLARE_TOP = 64.0       # where the neck has become the plain shaft

# rear fin
FIN_T0 = 3.2           # thickness at root
FIN_T1 = 0.8           # thickness at tip
FIN_Y1 = 32.0
FIN_Z0 = 41.0
FIN_Z1 = 38.5
FIN_R = 5.0

# blades
BLADE_T = 1.7
BLADE_H = 17.0
BLADE_TIP_X = 100.0
BLADE_ANG = 12.0       # deg, tips swept toward +Y
BLADE_TIP_R = 3.0
ROOT_D = 25.6          # where the rising root fillet meets the hood (distance from hood axis)
ROOT_FR = 20.0         # elevation root fillet radius
FLARE_D = 45.0         # where the plan root flare leaves the blade faces
FLARE_ANG = 22.4       # angular half width of the flare where it meets the hood (deg)

# webs filling the corners between the neck sides and the hood
WEB_H = 30.0
WEB_P1 = (COL_HX, 2.0)        # on the neck side
WEB_P2 = (20.6, -19.0)        # runs into the hood wall
WEB_TOP_X = (11.0, 11.5)      # where the sloping web face dies into the neck at WEB_H

# vertical rib inside the hood, in front of the neck
RIB_HW = 4.0
RIB_Y = -15.5
RIB_TOP = 54.0

# drive half-cylinder at the base
D_R = 7.4              # arch radius
D_ZC = 2.7             # arch centre height
D_HX = 18.2

# ---------------- hood ----------------
R_in = HOOD_R_OUT - HOOD_T


def hood_profile(r_bot, r_top, z0, extra_top=0.0):
    """closed (r, z) region from the axis out to a smooth wall profile"""
    zt = HOOD_TOP
    dr = r_bot - r_top
    pts = [(r_bot - 0.025 * dr, HOOD_Z_BEND),
           (r_bot - 0.25 * dr, 0.5 * (HOOD_Z_BEND + zt) + 2.0),
           (r_top, zt)]
    w = (
        cq.Workplane("XZ")
        .moveTo(0, z0)
        .lineTo(r_bot, z0)
    )
    if z0 < 0:
        w = w.lineTo(r_bot, 0.0)
    w = (
        w.spline(pts, tangents=[(0, 1), (-0.35, 1)], includeCurrent=True)
    )
    if extra_top > 0:
        w = w.lineTo(r_top - 0.35 * extra_top, zt + extra_top).lineTo(0, zt + extra_top)
    else:
        w = w.lineTo(0, zt)
    return w.close().revolve(360, (0, 0, 0), (0, 1, 0))


outer_solid = hood_profile(HOOD_R_OUT, HOOD_R_OUT_TOP, 0.0)
inner_solid = hood_profile(R_in, HOOD_R_OUT_TOP - HOOD_T, -5.0, extra_top=10.0)
# put the revolve seam into the opening (it is cut away)
outer_solid = outer_solid.rotate((0, 0, 0), (0, 0, 1), -90).translate((0, C_Y, 0))
inner_solid = inner_solid.rotate((0, 0, 0), (0, 0, 1), -90).translate((0, C_Y, 0))

hood = outer_solid.cut(inner_solid)

# opening wedge toward -Y
L = 100.0
a = math.radians(OPEN_HALF)
wedge = (
    cq.Workplane("XY")
    .workplane(offset=-5)
    .polyline([(0, C_Y), (L * math.sin(a), C_Y - L * math.cos(a)),
               (-L * math.sin(a), C_Y - L * math.cos(a))])
    .close()
    .extrude(HOOD_TOP + 20)
)
hood = hood.cut(wedge)

# side profile that rounds the top of the hood toward the open end
keep = (
    cq.Workplane("YZ")
    .moveTo(-70, -2)
    .lineTo(50, -2)
    .lineTo(50, HOOD_TOP + 5)
    .lineTo(TOP_FLAT_Y, HOOD_TOP + 5)
    .lineTo(TOP_FLAT_Y, HOOD_TOP)
    .spline(TOP_CURVE + [(END_Y, END_Z)],
            tangents=[(-1, 0), (-0.45, -1)], includeCurrent=True)
    .lineTo(-70, END_Z)
    .close()
    .extrude(80, both=True)
)
hood = hood.intersect(keep)

# ---------------- neck tapering into the shaft ----------------
def el_sketch(a, b, yc, z):
    # rotated by 90 deg so that the seam of the elliptic surfaces lies at the back (+Y)
    return cq.Sketch().ellipse(b, a, angle=90).moved(cq.Location(cq.Vector(0, yc, z)))


neck = (
    cq.Workplane("XY")
    .placeSketch(
        el_sketch(*NECK_BASE, 0.0),
        el_sketch(*NECK_MID, NECK_MID_Z),
        el_sketch(SHAFT_A, SHAFT_B, 0.0, FLARE_TOP),
    )
    .loft(combine=True)
)
# the neck is trimmed to a rounded block at its base (flat sides, flat back)
prism = (
    cq.Workplane("XY")
    .center(0, 0.5 * (COL_Y0 + COL_Y1))
    .rect(2 * COL_HX, COL_Y1 - COL_Y0)
    .extrude(FLARE_TOP)
    .edges("|Z").fillet(COL_R)
)
neck = neck.intersect(prism)

shaft = (
    cq.Workplane("XY")
    .placeSketch(el_sketch(SHAFT_A, SHAFT_B, 0.0, FLARE_TOP))
    .extrude(SHAFT_TOP - FLARE_TOP)
)

core = neck.union(shaft).cut(outer_solid)

# ---------------- rear fin ----------------
fin_side = (
    cq.Workplane("YZ")
    .moveTo(0, 0)
    .lineTo(FIN_Y1, 0)
    .lineTo(FIN_Y1, FIN_Z1 - FIN_R)
    .threePointArc((FIN_Y1 - FIN_R * (1 - math.cos(math.pi / 4)), FIN_Z1 - FIN_R * (1 - math.sin(math.pi / 4))),
                   (FIN_Y1 - FIN_R, FIN_Z1))
    .lineTo(0, FIN_Z0)
    .close()
    .extrude(5, both=True)
)
fin_plan = (
    cq.Workplane("XY")
    .polyline([(-FIN_T0 / 2, 0), (FIN_T0 / 2, 0), (FIN_T1 / 2, FIN_Y1 + 1), (-FIN_T1 / 2, FIN_Y1 + 1)])
    .close()
    .extrude(60)
)
fin = fin_side.intersect(fin_plan)

# ---------------- blades ----------------
d_tip = BLADE_TIP_X / math.cos(math.radians(BLADE_ANG))
fc_d = ROOT_D + ROOT_FR
# elevation of blade + root fillet, revolved about the hood axis so that the
# rising root blend also runs around the plan flares
c45 = math.cos(math.pi / 4)
blade_elev = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(d_tip, 0)
    .lineTo(d_tip, BLADE_H - BLADE_TIP_R)
    .threePointArc((d_tip - BLADE_TIP_R * (1 - c45), BLADE_H - BLADE_TIP_R * (1 - c45)),
                   (d_tip - BLADE_TIP_R, BLADE_H))
    .lineTo(fc_d, BLADE_H)
    .threePointArc((fc_d - ROOT_FR * c45, BLADE_H + ROOT_FR - ROOT_FR * c45),
                   (ROOT_D, BLADE_H + ROOT_FR))
    .lineTo(ROOT_D - 4.0, BLADE_H + ROOT_FR + 10.0)
    .lineTo(0, BLADE_H + ROOT_FR + 10.0)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

# plan outline with root flares: concave arcs tangent to the blade faces that
# run into the hood at an angle (like the moulded gussets of the original)
w1 = BLADE_T / 2
H = (HOOD_R_OUT * math.cos(math.radians(FLARE_ANG)), HOOD_R_OUT * math.sin(math.radians(FLARE_ANG)))
# arc radius so that the arc is tangent to w = w1 at d = FLARE_D and passes through H
rho_f = ((FLARE_D - H[0]) ** 2 + (H[1] - w1) ** 2) / (2 * (H[1] - w1))
cf = (FLARE_D, w1 + rho_f)
a_s = -math.pi / 2
a_h = math.atan2(H[1] - cf[1], H[0] - cf[0])
a_m = 0.5 * (a_s + a_h)
Mf = (cf[0] + rho_f * math.cos(a_m), cf[1] + rho_f * math.sin(a_m))
plan = (
    cq.Workplane("XY")
    .moveTo(0, 0)
    .lineTo(H[0], H[1])
    .threePointArc(Mf, (FLARE_D, w1))
    .lineTo(d_tip, w1)
    .lineTo(d_tip, -w1)
    .lineTo(FLARE_D, -w1)
    .threePointArc((Mf[0], -Mf[1]), (H[0], -H[1]))
    .close()
    .extrude(60)
)

blade = plan.intersect(blade_elev)
blade = blade.rotate((0, 0, 0), (0, 0, 1), BLADE_ANG).translate((0, C_Y, 0))
blade = blade.cut(outer_solid)
blade_l = blade.mirror("YZ")

# ---------------- drive half cylinders ----------------
dcyl = (
    cq.Workplane("YZ")
    .workplane(offset=-D_HX)
    .moveTo(-D_R, 0)
    .lineTo(D_R, 0)
    .lineTo(D_R, D_ZC)
    .threePointArc((0, D_ZC + D_R), (-D_R, D_ZC))
    .close()
    .extrude(2 * D_HX)
)

# ---------------- corner webs between neck and hood ----------------
web = (
    cq.Workplane("XY")
    .polyline([(9.0, WEB_P1[1]), WEB_P1, WEB_P2, (9.0, WEB_P2[1])]).close()
    .workplane(offset=WEB_H)
    .polyline([(9.0, WEB_P1[1]), (WEB_TOP_X[0], WEB_P1[1]), (WEB_TOP_X[1], WEB_P2[1]),
               (9.0, WEB_P2[1])]).close()
    .loft(combine=True, ruled=True)
)
web = web.cut(outer_solid)
web_l = web.mirror("YZ")

# ---------------- inner rib ----------------
rib = (
    cq.Workplane("XY")
    .center(0, 0.5 * (RIB_Y - 8.0))
    .rect(2 * RIB_HW, -8.0 - RIB_Y)
    .extrude(RIB_TOP)
    .edges("|Z and <Y").fillet(1.0)
)

result = (
    hood.union(core)
    .union(rib)
    .union(web)
    .union(web_l)
    .union(fin)
    .union(blade)
    .union(blade_l)
    .union(dcyl)
)
